import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 200.0          # plate size along X
D = 209.0          # plate size along Y
T = 12.0           # plate thickness
R_CORNER = 7.5     # plate vertical corner radius

H_LEG = 56.0       # leg height below the plate
LEG_X = 33.5       # leg size along X (outer face flush with plate X edge)
LEG_Y = 61.0       # leg size along Y
LEG_INSET_Y = 8.2  # inset of legs from the plate Y edges
WALL = 4.5         # leg side wall thickness
FLOOR = 4.0        # leg bottom wall thickness
END_WALL = 3.0     # leg outer (end) wall thickness

WIN = 27.7         # square window through the leg end wall
HOLE_PITCH = 39.0  # square pitch of the 4 fixing holes
HOLE_D = 6.0       # fixing hole diameter
PATTERN_Z = 30.5   # height of window / hole pattern centre above leg bottom

POCKET_X = 87.0    # shallow rectangular recess in plate underside
POCKET_Y = 128.0
POCKET_CY = -31.0  # recess centre offset along Y
POCKET_DEPTH = 2.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .workplane(offset=H_LEG)
    .rect(W, D)
    .extrude(T)
    .edges("|Z")
    .fillet(R_CORNER)
)

# shallow recess in the underside of the plate
pocket = (
    cq.Workplane("XY")
    .workplane(offset=H_LEG)
    .center(0, POCKET_CY)
    .rect(POCKET_X, POCKET_Y)
    .extrude(POCKET_DEPTH)
)
plate = plate.cut(pocket)


def make_leg(sx, sy):
    """Hollow leg: a box open toward the part centre (in X) with a closed
    bottom, two side walls and an outer end wall carrying a square window
    and four fixing holes."""
    x_out = sx * W / 2.0
    xc = x_out - sx * LEG_X / 2.0
    yc = sy * (D / 2.0 - LEG_INSET_Y - LEG_Y / 2.0)

    leg = (
        cq.Workplane("XY")
        .box(LEG_X, LEG_Y, H_LEG, centered=(True, True, False))
        .translate((xc, yc, 0))
    )

    # cavity (runs out through the inner X face and up to the plate)
    cav_len = LEG_X - END_WALL + 1.0
    cav_xc = x_out - sx * (END_WALL + cav_len / 2.0)
    cavity = (
        cq.Workplane("XY")
        .box(cav_len, LEG_Y - 2 * WALL, H_LEG - FLOOR + 1.0, centered=(True, True, False))
        .translate((cav_xc, yc, FLOOR))
    )
    leg = leg.cut(cavity)

    # window + 4 holes through the end wall
    zc = PATTERN_Z
    cut_len = END_WALL + 2.0
    x0 = x_out + sx * 1.0  # start just outside the end face, cut inward
    win = (
        cq.Workplane("XY")
        .box(cut_len, WIN, WIN)
        .translate((x0 - sx * cut_len / 2.0, yc, zc))
    )
    holes = None
    for dy in (-HOLE_PITCH / 2.0, HOLE_PITCH / 2.0):
        for dz in (-HOLE_PITCH / 2.0, HOLE_PITCH / 2.0):
            h = (
                cq.Workplane("YZ")
                .circle(HOLE_D / 2.0)
                .extrude(cut_len)
                .translate((x0 - (cut_len if sx > 0 else 0.0), yc + dy, zc + dz))
            )
            holes = h if holes is None else holes.union(h)
    leg = leg.cut(win).cut(holes)
    return leg


result = plate
for sx in (1, -1):
    for sy in (1, -1):
        # clean=False keeps the plate/leg face boundaries, as in the reference
        result = result.union(make_leg(sx, sy), clean=False)
